import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FLANGE_D = 100.0       # outer flange diameter
FLANGE_T = 7.5         # flange thickness
STEP_D = 84.6          # thin step ring diameter
STEP_T = 2.0           # step ring height
CUP_D = 72.0           # cup outer diameter
TOTAL_H = 20.5         # overall height (top of cup)

BORE_D = 58.0          # bowl bore diameter at the rim
HOLE_D = 32.8          # central through hole diameter
HOLE_LAND = 2.4        # height of the cylindrical part of the central hole
CONE_ANG = 30.0        # bowl floor cone angle from horizontal (deg)
BOWL_FILLET = 7.7      # fillet between bore wall and cone floor

BOLT_PCD = 84.0        # pitch circle of the two counterbored holes (on Y axis)
BOLT_D = 7.7           # through hole
CBORE_D = 15.0         # counterbore diameter
CBORE_FLOOR = 5.4      # counterbore floor height above the base
NOTCH_FILLET = 2.5     # rounding of the vertical edges where the counterbore
                       # cuts the cup wall and the step ring

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived values ----------------
R_f = FLANGE_D / 2
R_s = STEP_D / 2
R_c = CUP_D / 2
R_b = BORE_D / 2
R_h = HOLE_D / 2
z_step = FLANGE_T
z_cup = FLANGE_T + STEP_T

# corner between bore wall and cone floor, and fillet tangent points
a = math.radians(CONE_ANG)
zc = HOLE_LAND + (R_b - R_h) * math.tan(a)
u1 = (0.0, 1.0)                       # up the wall
u2 = (-math.cos(a), -math.sin(a))     # down the cone
ang = math.acos(u1[0] * u2[0] + u1[1] * u2[1])
t = BOWL_FILLET / math.tan(ang / 2)
P1 = (R_b + t * u1[0], zc + t * u1[1])
P2 = (R_b + t * u2[0], zc + t * u2[1])
bx, by = u1[0] + u2[0], u1[1] + u2[1]
bl = math.hypot(bx, by)
bx, by = bx / bl, by / bl
dc = BOWL_FILLET / math.sin(ang / 2)
Pm = (R_b + (dc - BOWL_FILLET) * bx, zc + (dc - BOWL_FILLET) * by)

# ---------------- stepped outer body (revolved) ----------------
def _revolve_rz(pts, seam_deg):
    """Revolve a closed (r, z) polyline about Z; seam placed at seam_deg."""
    wp = cq.Workplane("XZ").moveTo(*pts[0])
    for p in pts[1:]:
        wp = wp.lineTo(*p)
    return (
        wp.close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), seam_deg)
    )


flange = _revolve_rz(
    [(0, 0), (R_f, 0), (R_f, z_step), (0, z_step)], 45
)
upper = _revolve_rz(
    [(0, z_step - 0.5), (R_s, z_step - 0.5), (R_s, z_cup), (R_c, z_cup),
     (R_c, TOTAL_H), (0, TOTAL_H)], 90   # seam lies inside a counterbore
)
outer = flange.union(upper)

# ---------------- bowl + central hole (revolved cutter) ----------------
bowl = (
    cq.Workplane("XZ")
    .moveTo(0, -1)
    .lineTo(R_h, -1)
    .lineTo(R_h, HOLE_LAND)
    .lineTo(P2[0], P2[1])
    .threePointArc(Pm, P1)
    .lineTo(R_b, TOTAL_H + 1)
    .lineTo(0, TOTAL_H + 1)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), 45)
)
body = outer.cut(bowl)

# ---------------- counterbored holes at +/-Y ----------------
for sy in (1, -1):
    y = sy * BOLT_PCD / 2
    thru = (
        cq.Workplane("XY")
        .workplane(offset=-1)
        .center(0, y)
        .circle(BOLT_D / 2)
        .extrude(TOTAL_H + 2)
    )
    cb = (
        cq.Workplane("XY")
        .workplane(offset=CBORE_FLOOR)
        .center(0, y)
        .circle(CBORE_D / 2)
        .extrude(TOTAL_H)
    )
    body = body.cut(thru).cut(cb)


# round the vertical edges left where the counterbores cut the cup and step
def _notch_edge(e):
    c = e.Center()
    return (
        e.geomType() == "LINE"
        and c.z > z_step + 0.1
        and abs(abs(c.y) - BOLT_PCD / 2) < CBORE_D
        and abs(c.x) < CBORE_D
    )


notch_edges = [e for e in body.edges("|Z").vals() if _notch_edge(e)]
body = body.newObject(notch_edges).fillet(NOTCH_FILLET)

result = body
